import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# X = width, Y = depth (front flange at y=0, open back at y=DEPTH), Z = height
FL_W = 120.0        # flange width (X)
H = 88.0            # overall height (Z); flange and body flush top/bottom
FL_T = 5.0          # flange thickness (Y)
FL_R = 5.4          # flange corner radius (in XZ)
BODY_W = 94.5       # body width (X)
DEPTH = 44.2        # overall depth (Y) incl. flange
BODY_R = 1.2        # fillet on the body's long (Y-parallel) edges
WALL = 3.5          # side wall thickness
FRONT_T = 3.8       # front wall thickness (cavity floor at y = FRONT_T)

FL_HOLE_D = 4.5
FL_HOLE_X = 53.5    # +- from centre
FL_HOLE_Z = 31.3    # +- from centre

# lid screw posts in the cavity corners (short posts at the open rim)
# (x, z) of the four lid screw holes (measured; the +X pair sits tighter in the corner)
CP_HOLES = [(42.3, 39.0), (42.3, -37.6), (-40.4, 37.3), (-40.2, -36.7)]
CP_R = 3.8          # post radius around the hole
CP_LEN = 7.7        # post length from the rim
CP_HOLE_D = 3.0

# top wall openings
RECT_X0, RECT_X1 = -24.1, -7.5
RECT_Y0, RECT_Y1 = 14.8, 25.2
TOP_HOLE_X, TOP_HOLE_Y, TOP_HOLE_D = 3.2, 32.8, 3.5

# side (+X) hole
SIDE_HOLE_Y, SIDE_HOLE_Z, SIDE_HOLE_D = 32.0, 1.0, 4.5

# bottom big hole
BOT_HOLE_X, BOT_HOLE_Y, BOT_HOLE_D = 31.0, 29.5, 18.8

# internal PCB bosses (x, z) standing on the inner face of the front wall
BOSS_R = 5.3
BOSS_TOP = 17.2     # y of boss end faces
BOSS_HOLE_D = 3.0
BOSS_CH = 0.5       # chamfer on boss end faces
BOSS_HOLE_DEPTH = 9.0
BOSSES = [(35.1, 17.1), (9.5, 17.1), (35.1, -21.2), (9.4, -21.2), (-0.7, -32.7)]

# small locating block beside boss C (towards -X)
BLK_X0, BLK_X1 = 26.3, 31.0
BLK_Z0, BLK_Z1 = -22.8, -20.7
BLK_TOP = 10.75

# rib on boss E: straight rib from a point inside the boss to its tip (relative to boss E centre)
RIB_T = 2.0
RIB_BASE = (-0.3, 4.6)
RIB_TIP = (-4.9, 11.9)
WEB_FRAC = 0.55     # web under boss E, fraction of boss diameter
WEB_RECESS = 3.0    # web front face sits this far behind the boss face

IN_W = BODY_W - 2 * WALL
IN_H = H - 2 * WALL


def xz_prism(sketch_wp_fn, y0, y1):
    """helper: build a prism from a 2D profile on an XZ plane between y0 and y1 (y1 > y0)."""
    wp = cq.Workplane("XZ", origin=(0, y0, 0))
    return sketch_wp_fn(wp).extrude(-(y1 - y0))


# ---------------- flange ----------------
flange = (
    cq.Workplane("XZ")
    .rect(FL_W, H)
    .extrude(-FL_T)          # XZ normal is -Y; negative extrude goes +Y
    .edges("|Y")
    .fillet(FL_R)
)

# ---------------- body ----------------
body = (
    cq.Workplane("XZ")
    .rect(BODY_W, H)
    .extrude(-DEPTH)
    .edges("|Y")
    .fillet(BODY_R)
)

part = flange.union(body)

# ---------------- cavity (open at back) ----------------
cavity = (
    cq.Workplane("XZ", origin=(0, FRONT_T, 0))
    .rect(IN_W, IN_H)
    .extrude(-(DEPTH - FRONT_T + 1.0))
)
part = part.cut(cavity)

# ---------------- lid screw corner posts ----------------
for (cx, cz) in CP_HOLES:
    sx = 1 if cx > 0 else -1
    sz = 1 if cz > 0 else -1
    # rounded post filling the corner: a circle around the hole plus
    # rectangles tying it into the two adjacent walls
    post = xz_prism(lambda wp: wp.center(cx, cz).circle(CP_R), DEPTH - CP_LEN, DEPTH)
    wx = sx * (IN_W / 2 + 0.5)
    wz = sz * (IN_H / 2 + 0.5)
    tie_x = xz_prism(
        lambda wp: wp.center((cx + wx) / 2, cz).rect(abs(wx - cx), 2 * CP_R),
        DEPTH - CP_LEN, DEPTH)
    tie_z = xz_prism(
        lambda wp: wp.center(cx, (cz + wz) / 2).rect(2 * CP_R, abs(wz - cz)),
        DEPTH - CP_LEN, DEPTH)
    part = part.union(post).union(tie_x).union(tie_z)
    hole = xz_prism(lambda wp: wp.center(cx, cz).circle(CP_HOLE_D / 2),
                    DEPTH - CP_LEN + 1.0, DEPTH + 1.0)
    part = part.cut(hole)

# ---------------- internal bosses ----------------
for (bx, bz) in BOSSES:
    b = xz_prism(lambda wp: wp.center(bx, bz).circle(BOSS_R), FRONT_T - 0.5, BOSS_TOP)
    b = b.faces(">Y").edges().chamfer(BOSS_CH)
    part = part.union(b)
    h = xz_prism(lambda wp: wp.center(bx, bz).circle(BOSS_HOLE_D / 2),
                 BOSS_TOP - BOSS_HOLE_DEPTH, BOSS_TOP + 1.0)
    part = part.cut(h)

# locating block next to boss C
blk = xz_prism(
    lambda wp: wp.center((BLK_X0 + BLK_X1) / 2, (BLK_Z0 + BLK_Z1) / 2)
    .rect(BLK_X1 - BLK_X0, BLK_Z1 - BLK_Z0),
    FRONT_T - 0.5, BLK_TOP)
part = part.union(blk)

# web and rib on boss E (rib leaning towards -X)
ex, ez = BOSSES[4]
web_w = 2 * BOSS_R * WEB_FRAC
web = xz_prism(
    lambda wp: wp.center(ex, (ez + (-IN_H / 2 - 0.5)) / 2).rect(web_w, ez - (-IN_H / 2 - 0.5)),
    FRONT_T - 0.5, BOSS_TOP - WEB_RECESS)
part = part.union(web)
rdx, rdz = RIB_TIP[0] - RIB_BASE[0], RIB_TIP[1] - RIB_BASE[1]
rib_len = math.hypot(rdx, rdz)
rib_ang = math.degrees(math.atan2(-rdx, rdz))      # from +Z towards -X
rmx, rmz = ex + (RIB_BASE[0] + RIB_TIP[0]) / 2, ez + (RIB_BASE[1] + RIB_TIP[1]) / 2
rib = xz_prism(lambda wp: wp.center(rmx, rmz).rect(RIB_T, rib_len), FRONT_T - 0.5, BOSS_TOP)
# rect was built axis-aligned about its own centre; rotate it about that centre (axis // Y)
rib = rib.rotate((rmx, 0, rmz), (rmx, 1, rmz), -rib_ang)
part = part.union(rib)
# re-drill boss E hole (rib does not reach it, but keep clean)
part = part.cut(xz_prism(lambda wp: wp.center(ex, ez).circle(BOSS_HOLE_D / 2),
                         BOSS_TOP - BOSS_HOLE_DEPTH, BOSS_TOP + 1.0))

# ---------------- flange holes ----------------
for sx in (-1, 1):
    for sz in (-1, 1):
        h = xz_prism(lambda wp: wp.center(sx * FL_HOLE_X, sz * FL_HOLE_Z).circle(FL_HOLE_D / 2),
                     -1.0, FL_T + 1.0)
        part = part.cut(h)

# ---------------- top rectangular opening ----------------
rect = (
    cq.Workplane("XY", origin=((RECT_X0 + RECT_X1) / 2, (RECT_Y0 + RECT_Y1) / 2, H / 2 - WALL - 1))
    .rect(RECT_X1 - RECT_X0, RECT_Y1 - RECT_Y0)
    .extrude(WALL + 2)
)
part = part.cut(rect)

# top small hole
th = (
    cq.Workplane("XY", origin=(TOP_HOLE_X, TOP_HOLE_Y, H / 2 - WALL - 1))
    .circle(TOP_HOLE_D / 2)
    .extrude(WALL + 2)
)
part = part.cut(th)

# side hole (+X wall)
sh = (
    cq.Workplane("YZ", origin=(BODY_W / 2 - WALL - 1, SIDE_HOLE_Y, SIDE_HOLE_Z))
    .circle(SIDE_HOLE_D / 2)
    .extrude(WALL + 2)
)
part = part.cut(sh)

# bottom big hole
bh = (
    cq.Workplane("XY", origin=(BOT_HOLE_X, BOT_HOLE_Y, -H / 2 - 1))
    .circle(BOT_HOLE_D / 2)
    .extrude(WALL + 2)
)
part = part.cut(bh)

result = part
